import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 200.0          # plate length (X)
D = 90.0           # plate depth (Y)
T = 5.0            # plate thickness
R_CORNER = 2.0     # vertical corner radius of plate

WALL_T = 1.2       # wall thickness
WALL_IN = 1.6      # inset of wall outer face from plate edge
WALL_H = 4.1       # wall height above plate top
WALL_TOP_R = 0.0   # optional fillet on wall top edges (target: sharp)
WALL_END = 8.0     # distance from plate edge to wall ends (corner clearance)

GAP_C = 5.2        # x-centre of the gap in front/back walls
GAP_W = 26.0       # gap width

HOLE_D = 3.4       # perimeter hole diameter
CSK_D = 6.5        # countersink diameter (underside)
HOLE_OFF_X = 3.9   # corner hole offset from X edge
HOLE_OFF_Y = 4.05  # corner hole offset from Y edge
GAP_HOLE_X = (-3.9, 14.3)  # x of holes inside wall gap

BOSS_L = 20.0
BOSS_W = 10.0
BOSS_H = WALL_H
BOSS_X = 1.1
BOSS_HOLE_D = 4.5
BOSS_CSK_D = 8.0
BOSS_HOLE_SP = 10.0

PIN_D = 1.2
PIN_DEPTH = 3.0
PIN_HOLES = [(-81.9, 28.6), (-15.0, 28.6), (-76.0, -22.2), (-15.0, -22.2)]

# ---------------- base plate ----------------
plate = (cq.Workplane("XY").rect(W, D).extrude(T)
         .edges("|Z").fillet(R_CORNER))

# ---------------- walls ----------------
def box(x0, x1, y0, y1, h):
    b = (cq.Workplane("XY").workplane(offset=T)
         .center((x0 + x1) / 2, (y0 + y1) / 2)
         .rect(abs(x1 - x0), abs(y1 - y0)).extrude(h))
    return b if WALL_TOP_R <= 0 else b.faces(">Z").edges().fillet(WALL_TOP_R)

xo = W / 2 - WALL_IN
yo = D / 2 - WALL_IN
walls = []
# side walls (along Y at +-X)
for s in (-1, 1):
    x_out = s * xo
    x_in = s * (xo - WALL_T)
    walls.append(box(x_out, x_in, -D / 2 + WALL_END, D / 2 - WALL_END, WALL_H))
# front/back walls, two segments each
gx0 = GAP_C - GAP_W / 2
gx1 = GAP_C + GAP_W / 2
for s in (-1, 1):
    y_out = s * yo
    y_in = s * (yo - WALL_T)
    walls.append(box(-W / 2 + WALL_END, gx0, y_out, y_in, WALL_H))
    walls.append(box(gx1, W / 2 - WALL_END, y_out, y_in, WALL_H))

part = plate
for w in walls:
    part = part.union(w)

# ---------------- central boss ----------------
boss = (cq.Workplane("XY").workplane(offset=T).center(BOSS_X, 0)
        .rect(BOSS_L, BOSS_W).extrude(BOSS_H))
part = part.union(boss)

# ---------------- holes ----------------
per_pts = []
for sx in (-1, 1):
    for sy in (-1, 1):
        per_pts.append((sx * (W / 2 - HOLE_OFF_X), sy * (D / 2 - HOLE_OFF_Y)))
for gx in GAP_HOLE_X:
    for sy in (-1, 1):
        per_pts.append((gx, sy * (D / 2 - HOLE_OFF_Y)))

# countersunk from underside
part = (part.faces("<Z").workplane(centerOption="CenterOfBoundBox")
        .pushPoints([(x, -y) for x, y in per_pts])
        .cskHole(HOLE_D, CSK_D, 90))

boss_pts = [(BOSS_X - BOSS_HOLE_SP / 2, 0), (BOSS_X + BOSS_HOLE_SP / 2, 0)]
part = (part.faces("<Z").workplane(centerOption="CenterOfBoundBox")
        .pushPoints([(x, -y) for x, y in boss_pts])
        .cskHole(BOSS_HOLE_D, BOSS_CSK_D, 90))

# small blind holes from the top
pins = (cq.Workplane("XY").workplane(offset=T - PIN_DEPTH)
        .pushPoints(PIN_HOLES).circle(PIN_D / 2).extrude(PIN_DEPTH + 0.1))
part = part.cut(pins)

result = part
VIEW = {"azimuth": 45, "elevation": 26}
